import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
SO_R = 4.75           # standoff outer radius
SO_HOLE_D = 4.5       # standoff through-hole diameter
CX = 55.25            # standoff centre offset from part centre in X
CY_SPACING = 86.8     # standoff centre spacing in Y (front to back)
H = 45.2              # overall height (standoffs and front panel)
FLOOR_T = 3.5         # floor plate thickness
FLOOR_SIDE_INSET = 0.25  # floor side faces sit just inside the post tangents
WALL_T = 2.4          # front panel thickness
WALL_END_INSET = 1.0  # panel ends this far inboard of the standoff centres
LIP_D = 2.2           # projection of the sloped lip on the back edge
INNER_HALF = 4.15     # inboard flat of the front standoffs, from the post axis

# vent pattern on the front panel
N_ROWS = 9
N_COLS = 10           # diamonds per row
HALF_PITCH = 4.77     # horizontal offset between neighbouring rows
ROW_PITCH = 4.18      # vertical distance between rows
PAT_ZC = 23.2         # height of the pattern centre
DIA_W = 5.85          # diamond width (across X)
DIA_H = 5.25          # diamond height (across Z)
DOT_X = 47.8          # x position of the small holes at row ends
DOT_W = 1.45          # small diamond width
DOT_H = 1.3           # small diamond height

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
yf = -CY_SPACING / 2.0          # front standoff centre y
yb = CY_SPACING / 2.0           # back standoff centre y
y_wall_in = yf - SO_R           # panel inner face
y_wall_out = y_wall_in - WALL_T  # panel outer face
wall_x = CX - WALL_END_INSET

# ---------------- floor plate ----------------
# The floor is a rounded rectangle whose corner arcs are the standoffs themselves:
# build it as a cross of two rectangles and let the standoff posts fill the corners.
floor_a = (
    cq.Workplane("XY")
    .center(0, (yf + yb) / 2.0)
    .rect(2 * (CX + SO_R - FLOOR_SIDE_INSET), CY_SPACING)
    .extrude(FLOOR_T)
)
floor_b = (
    cq.Workplane("XY")
    .center(0, (yf + yb) / 2.0)
    .rect(2 * CX, CY_SPACING + 2 * SO_R)
    .extrude(FLOOR_T)
)
floor = floor_a.union(floor_b)

# ---------------- front panel ----------------
wall = (
    cq.Workplane("XY")
    .box(2 * wall_x, WALL_T, H, centered=(True, False, False))
    .translate((0, y_wall_out, 0))
)

# ---------------- back standoffs ----------------
# plain tubes; the cylinder seam is turned toward -X/+Y (out of most views)
def post(x, y, seam_deg):
    return (
        cq.Workplane("XY")
        .circle(SO_R)
        .extrude(H)
        .rotate((0, 0, 0), (0, 0, 1), seam_deg)
        .translate((x, y, 0))
    )


back_posts = post(-CX, yb, 135.0).union(post(CX, yb, 135.0))

# ---------------- front standoffs ----------------
# Post circle joined to the panel end: a flat tangent to the panel's outer
# corner on the outboard side and a straight flat down to the panel on the
# inboard side.
cxl = -CX
P = (cxl + WALL_END_INSET, y_wall_out)         # outer corner of panel end
dx, dy = P[0] - cxl, P[1] - yf
dist = math.hypot(dx, dy)
phi = math.atan2(dy, dx)
ang_t = phi - math.acos(SO_R / dist)          # tangent point on the outboard side
T = (cxl + SO_R * math.cos(ang_t), yf + SO_R * math.sin(ang_t))
ang_i = -math.acos(INNER_HALF / SO_R)         # where the inboard flat meets the circle
I = (cxl + INNER_HALF, yf + SO_R * math.sin(ang_i))
a0 = ang_t if ang_t > 0 else ang_t + 2 * math.pi
ang_mid = (a0 + ang_i) / 2.0
M = (cxl + SO_R * math.cos(ang_mid), yf + SO_R * math.sin(ang_mid))

front_left = (
    cq.Workplane("XY")
    .moveTo(*P)
    .lineTo(*T)
    .threePointArc(M, I)
    .lineTo(cxl + INNER_HALF, y_wall_out)
    .close()
    .extrude(H)
)
front_right = front_left.mirror("YZ")

# ---------------- back sloped lip ----------------
lip = (
    cq.Workplane("YZ", origin=(-wall_x, 0, 0))
    .polyline([(yb + SO_R, 0), (yb + SO_R + LIP_D, 0), (yb + SO_R, FLOOR_T)])
    .close()
    .extrude(2 * wall_x)
)

body = floor.union(wall).union(back_posts).union(front_left).union(front_right).union(lip)

# ---------------- standoff through holes ----------------
holes = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .pushPoints([(-CX, yf), (CX, yf), (-CX, yb), (CX, yb)])
    .circle(SO_HOLE_D / 2.0)
    .extrude(H + 2)
)
body = body.cut(holes)

# ---------------- vent pattern ----------------
y_wall_mid = (y_wall_in + y_wall_out) / 2.0
x0 = -(2 * N_COLS - 1) * HALF_PITCH / 2.0
diamond_pts = []
dot_pts = []
for r in range(N_ROWS):
    z = PAT_ZC + (N_ROWS - 1) / 2.0 * ROW_PITCH - r * ROW_PITCH
    type_a = (r % 2 == 0)
    xs = x0 + (HALF_PITCH if type_a else 0.0)
    for c in range(N_COLS):
        diamond_pts.append((xs + 2 * HALF_PITCH * c, z))
    dot_pts.append((-DOT_X if type_a else DOT_X, z))

cutter = cq.Workplane("XZ", origin=(0, y_wall_mid, 0))
for (x, z) in diamond_pts:
    cutter = cutter.polyline(
        [(x - DIA_W / 2, z), (x, z + DIA_H / 2), (x + DIA_W / 2, z), (x, z - DIA_H / 2)]
    ).close()
cutter = cutter.extrude(WALL_T * 2, both=True)

dots = cq.Workplane("XZ", origin=(0, y_wall_mid, 0))
for (x, z) in dot_pts:
    dots = dots.polyline(
        [(x - DOT_W / 2, z), (x, z + DOT_H / 2), (x + DOT_W / 2, z), (x, z - DOT_H / 2)]
    ).close()
dots = dots.extrude(WALL_T * 2, both=True)

result = body.cut(cutter).cut(dots)
